import cadquery as cq

# --- driving dimensions (mm) ---
BLOCK_W = 60.0      # X
BLOCK_H = 44.8      # Z
BLOCK_D = 26.7      # Y (depth)
BLOCK_FILLET = 0.8

STEM_S = 22.3       # square stem side
STEM_L = 35.8       # stem length (toward -Y)
STEM_EDGE_R = 2.0   # long-edge fillet
STEM_END_R = 2.0    # end-face fillet

POCKET_S = 15.0     # square pocket on back face
POCKET_R = 1.5
POCKET_DEPTH = 20.0

# block: front face at Y=0, back face at Y=BLOCK_D
block = (
    cq.Workplane("XY")
    .box(BLOCK_W, BLOCK_D, BLOCK_H)
    .translate((0, BLOCK_D / 2.0, 0))
    .edges()
    .fillet(BLOCK_FILLET)
)

# square stem protruding toward -Y
stem = (
    cq.Workplane("XZ")
    .rect(STEM_S, STEM_S)
    .extrude(STEM_L + 0.5)      # XZ normal is -Y, so extrude goes to -Y
    .edges("|Y")
    .fillet(STEM_EDGE_R)
    .faces("<Y")
    .edges()
    .fillet(STEM_END_R)
)
# overlap slightly into block for a clean union
stem = stem.translate((0, 0.5, 0))

body = block.union(stem)

# square pocket on back face
pocket = (
    cq.Workplane("XZ", origin=(0, BLOCK_D, 0))
    .sketch()
    .rect(POCKET_S, POCKET_S)
    .vertices()
    .fillet(POCKET_R)
    .finalize()
    .extrude(POCKET_DEPTH)
)
result = body.cut(pocket)

VIEW = {"azimuth": 45, "elevation": 26}
